import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Servo + U-bracket (hinge frame) assembly, modelled as one solid.
# X = servo width, Y = servo length (bracket at -Y), Z = up.
# ---------------------------------------------------------------------------

# ---- servo body -----------------------------------------------------------
SW = 28.5            # servo width (X)
SY0, SY1 = 5.2, 57.2 # servo body Y extent
SH = 35.0            # servo height (Z)
CAP_Z = 11.9         # parting line of top/bottom caps
R_END_V = 4.4        # vertical edge rounding at the +Y end
R_END_H = 3.8        # rounding of the top/bottom cap edges

# servo horn / idler
HORN_Y = 45.2
HORN_D = 11.6
HORN_H = 3.2

# mounting tabs along the servo sides
TAB_YS = [11.15, 20.25, 29.25, 38.2]
TAB_L = 8.4          # length along Y
TAB_OUT = 3.5        # protrusion beyond the side
TAB_H = 5.6          # height (Z)

# end plate between servo and bracket
EP_Y0, EP_Y1 = -0.15, 7.0
EP_HZ = 20.8
EP_HX = 13.75

# ---- bracket --------------------------------------------------------------
BW = 13.75           # bracket half width (X)
BZ = 26.45           # bracket half height (outer)
ARM_T = 3.65         # arm thickness
BASE_Y0, BASE_Y1 = -7.7, -0.1
IN_FIL = 7.0         # concave gusset radius under the top arm
LOW_FIL = 10.0       # concave gusset radius above the bottom arm
OUT_CH_Y = 5.5       # outer chamfer (Y)
OUT_CH_Z = 6.5       # outer chamfer (Z)

ARM_CX, ARM_CY = 16.25, -25.5   # horn axis
ARM_R = 12.0                    # rounded arm end radius
ARM_LEFT_Y = -20.3              # where the -X edge starts to slant
ARM_RIGHT_Y = -4.66             # where the +X edge starts to slant

HOLE_PCD_R = 8.8                # horn screw pattern radius
CB_D, CB_DEPTH = 4.8, 1.6       # horn screw counterbores

HEX_COLS = [-8.85, 0.0, 8.85]
HEX_ROWS = [17.8, 8.9, 0.0, -8.9, -17.8]
HEX_AF_OUT = 6.7
HEX_AF_NUT = 4.4


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_z(cx, cy, z0, h, d):
    return cq.Workplane("XY").workplane(offset=z0).center(cx, cy).circle(d / 2.0).extrude(h)


def hex_prism_y(cx, cz, y0, depth, af):
    # hexagonal prism with axis along Y, flat top (vertices on X axis)
    d_corners = af / math.cos(math.radians(30))
    return (cq.Workplane("XZ", origin=(0, y0, 0))
            .center(cx, cz)
            .polygon(6, d_corners)
            .extrude(-depth))


# ===========================================================================
# SERVO
# ===========================================================================
# rounded +Y end; the top/bottom cap edges are rounded along the sides too
servo = box(-SW / 2, SW / 2, SY0, SY1, -SH / 2, SH / 2)
servo = servo.edges("|Z and >Y").fillet(R_END_V)
servo = servo.faces(">Z or <Z").edges("not <Y").fillet(R_END_H)

# shallow parting grooves
for zc in (CAP_Z, -CAP_Z):
    g = box(-SW / 2 - 1, SW / 2 + 1, SY0 + 8.5, SY1 + 1, zc - 0.2, zc + 0.2)
    inner = box(-SW / 2 + 0.3, SW / 2 - 0.3, SY0, SY1 - 0.3, zc - 0.3, zc + 0.3)
    servo = servo.cut(g.cut(inner))

# horn on top
horn = cyl_z(0, HORN_Y, SH / 2, HORN_H, HORN_D).faces(">Z").edges().chamfer(0.6)
horn = horn.cut(cyl_z(0, HORN_Y, SH / 2 + HORN_H - 0.8, 1.0, 7.5))
horn = horn.union(cyl_z(0, HORN_Y, SH / 2 + HORN_H - 0.8, 0.8, 5.2))
horn = horn.cut(cyl_z(0, HORN_Y, SH / 2 + HORN_H - 1.5, 2.0, 2.6))
servo = servo.union(horn)

# idler boss underneath
idler = cyl_z(0, HORN_Y, -SH / 2 - 0.5, 0.5, 12.0)
idler = idler.union(cyl_z(0, HORN_Y, -SH / 2 - 2.8, 2.8, 6.0))
idler = idler.cut(cyl_z(0, HORN_Y, -SH / 2 - 3.0, 1.5, 2.4))
servo = servo.union(idler)

# bottom pad
PAD_T = 3.2
pad = box(-13.6, 13.6, 9.4, 36.6, -SH / 2 - PAD_T, -SH / 2 + 0.1)
pad = pad.faces("<Z").edges().chamfer(1.4)
pad = pad.cut(box(-7, 7, 15, 29, -SH / 2 - PAD_T - 0.3, -SH / 2 - PAD_T + 0.2))
servo = servo.union(pad)

# connector pockets on top
servo = servo.cut(box(-10.75, 10.75, 24.2, 31.4, SH / 2 - 2.4, SH / 2 + 1))
servo = servo.union(box(-0.45, 0.45, 24.2, 31.4, SH / 2 - 2.5, SH / 2))
for xc in (-5.35, 5.35):
    # connector housing with a latch ledge and three pin holes
    servo = servo.union(box(xc - 4.3, xc + 4.3, 24.2, 26.4, SH / 2 - 2.5, SH / 2 - 0.9))
    for k in (-1, 0, 1):
        servo = servo.cut(cyl_z(xc + 2.0 * k, 25.3, SH / 2 - 2.0, 1.5, 0.7))

# latch blocks on top near the bracket end
for (x0, x1) in ((-11.1, -4.3), (4.3, 11.1)):
    blk = box(x0, x1, 9.2, 17.2, SH / 2 - 0.1, EP_HZ)
    blk = blk.faces(">Z").edges().fillet(1.2)
    servo = servo.union(blk)

# small top holes
for (hx, hy) in ((-7.0, 53.0), (7.0, 53.0), (-8.8, 38.2), (8.9, 38.2),
                 (-8.8, 20.7), (8.8, 20.7)):
    servo = servo.cut(cyl_z(hx, hy, SH / 2 - 1.5, 2.0, 1.4))

# mounting tabs (top and bottom rows on both sides)
for side in (1, -1):
    for ty in TAB_YS:
        for top in (True, False):
            z0 = SH / 2 - TAB_H if top else -SH / 2
            z1 = z0 + TAB_H
            xa = side * (SW / 2 - 0.5)
            xb = side * (SW / 2 + TAB_OUT)
            tab = box(min(xa, xb), max(xa, xb), ty - TAB_L / 2, ty + TAB_L / 2, z0, z1)
            sel = ">Z"  # bevel on the upper outer edge for both rows
            selx = (">X" if side > 0 else "<X")
            tab = tab.edges(sel).edges(selx).chamfer(1.0 if top else 1.4)
            # nut slot open to the outside and to the cap side
            px0 = side * (SW / 2 + 1.2)
            px1 = side * (SW / 2 + TAB_OUT + 1)
            if top:
                pz0, pz1 = z0 - 1, z1 - 1.6
            else:
                pz0, pz1 = z0 + 1.6, z1 + 1
            tab = tab.cut(box(min(px0, px1), max(px0, px1),
                              ty - 2.5, ty + 2.5, pz0, pz1))
            # screw hole through the tab
            hz0 = SH / 2 - 2.0 if top else -SH / 2 - 0.5
            tab = tab.cut(cyl_z(side * (SW / 2 + 0.7), ty, hz0, 2.5, 1.6))
            servo = servo.union(tab)

# vertical corner posts at the bracket end of the servo (between tab rows)
for side in (1, -1):
    xa, xb = side * (SW / 2 - 1.0), side * (SW / 2 + TAB_OUT - 0.3)
    # full height post on +X, only at the tab rows on -X
    spans = [(-SH / 2, SH / 2)] if side > 0 else [(SH / 2 - TAB_H, SH / 2),
                                                  (-SH / 2, -SH / 2 + TAB_H)]
    for (pz0, pz1) in spans:
        post = box(min(xa, xb), max(xa, xb), EP_Y0, 7.0, pz0, pz1)
        post = post.edges("|Z and <Y and " + (">X" if side > 0 else "<X")).fillet(2.6)
        xo = max(abs(xa), abs(xb))
        for zs in (1, -1):
            zt = zs * SH / 2
            if not (pz0 - 0.01 <= zt <= pz1 + 0.01):
                continue
            cx_ = (cq.Workplane("XZ", origin=(0, 10, 0))
                   .polyline([(side * (xo - 1.6), zt + zs * 0.01), (side * (xo + 1), zt + zs * 0.01),
                              (side * (xo + 1), zt - zs * 2.6)]).close().extrude(12))
            cy_ = (cq.Workplane("YZ", origin=(-20, 0, 0))
                   .polyline([(EP_Y0 + 1.6, zt + zs * 0.01), (EP_Y0 - 1, zt + zs * 0.01),
                              (EP_Y0 - 1, zt - zs * 2.6)]).close().extrude(40))
            post = post.cut(cx_).cut(cy_)
        servo = servo.union(post)

# end plate between servo and bracket
ep = box(-EP_HX, EP_HX, EP_Y0, EP_Y1, -EP_HZ, EP_HZ)
ep = ep.faces("<Y").edges("|X").chamfer(1.0)
ep = ep.edges("|Z and >Y").chamfer(1.5)
servo = servo.union(ep)
# latches reaching into the bracket windows
for zs in (1, -1):
    lt = box(-3.8, 3.8, -1.6, EP_Y0 + 0.2, 16.1 if zs > 0 else -20.0,
             20.0 if zs > 0 else -16.1)
    lt = lt.edges("|X and <Y").chamfer(0.6)
    lt = lt.cut(box(-1.0, 1.0, -1.7, -0.9, -30, 30))
    servo = servo.union(lt)
for xc in (-8.6, 8.6):
    for zs in (1, -1):
        z0 = EP_HZ if zs > 0 else -EP_HZ - 0.8
        boss = cyl_z(xc, 5.2, z0, 0.8, 4.3)
        boss = boss.cut(cyl_z(xc, 5.2, z0 - 0.5, 2.0, 1.8))
        servo = servo.union(boss)

# ===========================================================================
# BRACKET
# ===========================================================================

def arm_outline():
    # tangent point from the slanted -X edge to the end circle
    px, py = -BW, ARM_LEFT_Y
    dx, dy = ARM_CX - px, ARM_CY - py
    d = math.hypot(dx, dy)
    ang = math.atan2(dy, dx) - math.asin(ARM_R / d)
    tl = math.sqrt(d * d - ARM_R * ARM_R)
    tlx, tly = px + tl * math.cos(ang), py + tl * math.sin(ang)
    # tangent point from the slanted +X edge
    qx, qy = BW, ARM_RIGHT_Y
    dx2, dy2 = ARM_CX - qx, ARM_CY - qy
    d2 = math.hypot(dx2, dy2)
    ang2 = math.atan2(dy2, dx2) + math.asin(ARM_R / d2)
    tl2 = math.sqrt(d2 * d2 - ARM_R * ARM_R)
    trx, try_ = qx + tl2 * math.cos(ang2), qy + tl2 * math.sin(ang2)
    # mid point of the arc (furthest toward -Y/+X)
    a1 = math.atan2(tly - ARM_CY, tlx - ARM_CX)
    a2 = math.atan2(try_ - ARM_CY, trx - ARM_CX)
    if a2 < a1:
        a2 += 2 * math.pi
    am = 0.5 * (a1 + a2)
    mx, my = ARM_CX + ARM_R * math.cos(am), ARM_CY + ARM_R * math.sin(am)
    return (cq.Workplane("XY")
            .moveTo(-BW, BASE_Y1)
            .lineTo(-BW, ARM_LEFT_Y)
            .lineTo(tlx, tly)
            .threePointArc((mx, my), (trx, try_))
            .lineTo(BW, ARM_RIGHT_Y)
            .lineTo(BW, BASE_Y1)
            .close())


arm_top = arm_outline().extrude(ARM_T).translate((0, 0, BZ - ARM_T))
arm_bot = arm_outline().extrude(ARM_T).translate((0, 0, -BZ))
bracket = arm_top.union(arm_bot)

# --- base: open lattice between two side rims ------------------------------
ZI = BZ - ARM_T          # inner face of the arms
LAT_Y = -2.8             # front face of the thin back plate
CEN_Y = -4.9             # front face of the recessed centre column
HEX_Y = -6.3             # front face of the hex bosses (behind rims / ribs)
RIM_T = 1.75
RIB_T = 1.05
RIB_X_END, RIB_X_MID = 5.9, 4.25
SMALL_FIL = 2.2          # small root gusset across the lattice


def u_profile(x0, x1, fil=IN_FIL, y_front=BASE_Y0, big=0.0):
    """Web with the U-bracket inner profile: base plus concave root gussets
    (radius `fil` under the top arm, radius `big` above the bottom arm)."""
    w = box(x0, x1, y_front, BASE_Y1, -ZI - 0.01, ZI + 0.01)
    for zs in (1, -1):
        r = big if (zs < 0 and big > 0) else fil
        zc = zs * (ZI - r)
        g = box(x0, x1, y_front - r, y_front + 0.01,
                min(zs * (ZI + 0.01), zc), max(zs * (ZI + 0.01), zc))
        c = (cq.Workplane("YZ").workplane(offset=x0 - 1)
             .center(y_front - r, zc).circle(r).extrude(x1 - x0 + 2))
        w = w.union(g.cut(c))
    return w


lat = u_profile(-BW, -BW + RIM_T, big=LOW_FIL)          # -X rim
lat = lat.union(u_profile(BW - RIM_T, BW, fil=SMALL_FIL))  # +X rim
lat = lat.union(box(-BW + 0.5, BW - 0.5, LAT_Y, BASE_Y1, -ZI - 0.01, ZI + 0.01))
# small root fillets across the side columns
for (x0, x1) in ((-BW, -RIB_X_END), (RIB_X_END, BW)):
    lat = lat.union(u_profile(x0, x1, fil=SMALL_FIL).cut(
        box(x0 - 1, x1 + 1, BASE_Y0 - 1, BASE_Y1 + 1, -ZI + SMALL_FIL, ZI - SMALL_FIL)))

# curved ribs either side of the centre column (sweep into the arms)
for sgn in (1, -1):
    pts = [(RIB_X_END, ZI + 0.5), (RIB_X_END, 14.6), (RIB_X_MID, 12.3),
           (RIB_X_MID, -12.3), (RIB_X_END, -14.6), (RIB_X_END, -ZI - 0.5)]
    left = [(sgn * (x - RIB_T / 2), z) for (x, z) in pts]
    right = [(sgn * (x + RIB_T / 2), z) for (x, z) in reversed(pts)]
    band = (cq.Workplane("XZ", origin=(0, BASE_Y1, 0))
            .polyline(left + right).close().extrude(LOW_FIL + 9.0))
    lat = lat.union(band.intersect(u_profile(-BW, BW, big=LOW_FIL)))

# recessed centre column
lat = lat.union(box(-RIB_X_MID, RIB_X_MID, CEN_Y, LAT_Y + 0.01, -ZI - 0.01, ZI + 0.01))

# hex bosses with nut pockets
for cx in HEX_COLS:
    for cz in HEX_ROWS:
        if cx == 0.0 and cz in (17.8, 0.0, -17.8):
            continue
        boss = hex_prism_y(cx, cz, HEX_Y, LAT_Y - HEX_Y + 0.01, HEX_AF_OUT)
        # trim the boss to its column (between rim and rib)
        if cx < 0:
            lim = box(-BW, -RIB_X_MID, BASE_Y0 - 1, BASE_Y1, -BZ, BZ)
        elif cx > 0:
            lim = box(RIB_X_MID, BW, BASE_Y0 - 1, BASE_Y1, -BZ, BZ)
        else:
            lim = box(-RIB_X_MID, RIB_X_MID, BASE_Y0 - 1, BASE_Y1, -BZ, BZ)
        lat = lat.union(boss.intersect(lim))
        lat = lat.cut(hex_prism_y(cx, cz, HEX_Y - 0.01, 1.6, HEX_AF_NUT))
        hole = (cq.Workplane("XZ", origin=(0, HEX_Y, 0)).center(cx, cz)
                .circle(1.2).extrude(-8))
        lat = lat.cut(hole)
        if abs(cz) < 17:
            # screw head inside the nut pocket
            lat = lat.union(
                cq.Workplane("XZ", origin=(0, HEX_Y + 1.6, 0)).center(cx, cz)
                .circle(1.8).extrude(0.6))

# chamfer along the front edge of the +X rim (below the arms)
rim_cut = (cq.Workplane("XY").workplane(offset=-ZI + 0.01)
           .polyline([(BW + 0.5, BASE_Y0 - IN_FIL - 0.1),
                      (BW - RIM_T - 0.5, BASE_Y0 - IN_FIL - 0.1),
                      (BW - RIM_T - 0.5, BASE_Y0 - 0.01 - 0.5),
                      (BW - RIM_T, BASE_Y0 - 0.01),
                      (BW + 0.01, -2.7), (BW + 0.5, -2.7)]).close()
           .extrude(2 * ZI - 0.02))
bracket = bracket.union(lat)

# outer block of the base behind the arms (full width) for the chamfer corners
bracket = bracket.union(box(-BW, BW, BASE_Y0, BASE_Y1, ZI - 0.01, BZ))
bracket = bracket.union(box(-BW, BW, BASE_Y0, BASE_Y1, -BZ, -ZI + 0.01))
bracket = bracket.cut(rim_cut)

# outer chamfers at base / arm corners
for zs in (1, -1):
    tri = (cq.Workplane("YZ").workplane(offset=-BW - 1)
           .polyline([(BASE_Y1 + 0.01, zs * (BZ + 0.01)),
                      (BASE_Y1 - OUT_CH_Y, zs * (BZ + 0.01)),
                      (BASE_Y1 + 0.01, zs * (BZ - OUT_CH_Z))]).close()
           .extrude(2 * BW + 2))
    bracket = bracket.cut(tri)

# centre column windows (through the lattice)
WIN_X = RIB_X_END - RIB_T / 2 - 0.02
bracket = bracket.cut(box(-3.15, 3.15, BASE_Y0 - 1, BASE_Y1 + 0.1, -5.4, 5.2))
# top window continues up through the chamfered arm root
bracket = bracket.cut(box(-WIN_X, WIN_X, BASE_Y0 - IN_FIL - 1, BASE_Y1 + 0.1, 14.6, ZI + 0.01))
bracket = bracket.cut(box(-WIN_X, WIN_X, BASE_Y1 - OUT_CH_Y + 0.3, BASE_Y1 + 0.1, ZI, BZ + 1))
bracket = bracket.cut(box(-WIN_X, WIN_X, BASE_Y0 - IN_FIL - 1, BASE_Y1 + 0.1, -ZI - 0.01, -14.6))

# small hole on the top arm
bracket = bracket.cut(cyl_z(-1.6, -17.1, BZ - ARM_T - 0.1, ARM_T + 0.2, 1.4))

# --- top arm horn (upper side): raised ring + 4 counterbored holes --------
top_ring = cyl_z(ARM_CX, ARM_CY, BZ, 1.45, 10.2)
bracket = bracket.union(top_ring)
bracket = bracket.cut(cyl_z(ARM_CX, ARM_CY, BZ + 0.6, 1.0, 6.2))
bracket = bracket.cut(cyl_z(ARM_CX, ARM_CY, BZ - ARM_T - 0.1, ARM_T + 2, 3.0))
centre_head = cyl_z(ARM_CX, ARM_CY, BZ + 0.6, 0.5, 4.6).cut(
    cq.Workplane("XY").workplane(offset=BZ + 0.7).center(ARM_CX, ARM_CY)
    .rect(2.6, 0.6).extrude(0.5).union(
        cq.Workplane("XY").workplane(offset=BZ + 0.7).center(ARM_CX, ARM_CY)
        .rect(0.6, 2.6).extrude(0.5)))
bracket = bracket.union(centre_head)
for k in range(4):
    a = k * math.pi / 2
    hx = ARM_CX + HOLE_PCD_R * math.cos(a)
    hy = ARM_CY + HOLE_PCD_R * math.sin(a)
    bracket = bracket.cut(cyl_z(hx, hy, BZ - CB_DEPTH, CB_DEPTH + 0.1, CB_D))
    bracket = bracket.cut(cyl_z(hx, hy, BZ - ARM_T - 0.1, ARM_T + 0.2, 2.3))
    # same pattern on the underside of the bottom arm
    bracket = bracket.cut(cyl_z(hx, hy, -BZ - 0.1, CB_DEPTH + 0.1, CB_D))
    bracket = bracket.cut(cyl_z(hx, hy, -BZ - 0.1, ARM_T + 0.2, 2.3))
    # socket-head screws sitting in the counterbores (top and bottom)
    for zs in (1, -1):
        zf = zs * (BZ - CB_DEPTH)            # counterbore floor
        head = cyl_z(hx, hy, zf if zs > 0 else zf - 0.9, 0.9, 3.8)
        sock = (cq.Workplane("XY").workplane(offset=(zf + 0.4) if zs > 0 else (zf - 1.3))
                .center(hx, hy).polygon(6, 1.7).extrude(0.9))
        bracket = bracket.union(head.cut(sock))

# --- top arm underside: horn disc + hub + pin ------------------------------
zt = BZ - ARM_T
bracket = bracket.union(cyl_z(ARM_CX, ARM_CY, zt - 2.1, 2.1, 13.0))
bracket = bracket.union(cyl_z(ARM_CX, ARM_CY, zt - 3.05, 1.0, 8.8))
bracket = bracket.union(cyl_z(ARM_CX, ARM_CY, zt - 5.85, 2.85, 2.6))

# --- bottom arm upper side: idler ring with blocks, nuts, hub + pin -------
zb = -BZ + ARM_T
IDL_H = 4.15
ring = cyl_z(ARM_CX, ARM_CY, zb, IDL_H, 2 * ARM_R).cut(
    cyl_z(ARM_CX, ARM_CY, zb - 0.1, IDL_H + 1, 2 * ARM_R - 3.0))
ring = ring.cut(box(ARM_CX - 0.5, ARM_CX + 0.5, ARM_CY - ARM_R - 1, ARM_CY - ARM_R + 2,
                    zb + 0.8, zb + IDL_H + 1)
                .rotate((ARM_CX, ARM_CY, 0), (ARM_CX, ARM_CY, 1), -30))
bracket = bracket.union(ring)
hub = cyl_z(ARM_CX, ARM_CY, zb, 7.15, 9.7)
hub = hub.cut(cyl_z(ARM_CX, ARM_CY, zb + 5.6, 2.0, 6.4))
bracket = bracket.union(hub)
bracket = bracket.union(cyl_z(ARM_CX, ARM_CY, zb + 5.5, 4.6, 2.6))
for k in range(4):
    # radial blocks on the diagonals
    a = math.degrees(k * math.pi / 2 + math.pi / 4)
    blk = (box(ARM_CX + 4.5, ARM_CX + ARM_R - 2.1, ARM_CY - 2.1, ARM_CY + 2.1,
               zb, zb + IDL_H - 0.4)
           .rotate((ARM_CX, ARM_CY, 0), (ARM_CX, ARM_CY, 1), a))
    bracket = bracket.union(blk)
    # hex nuts seated between the blocks
    b = k * math.pi / 2
    nx, ny = ARM_CX + 7.3 * math.cos(b), ARM_CY + 7.3 * math.sin(b)
    nut = (cq.Workplane("XY").workplane(offset=zb).center(nx, ny)
           .polygon(6, 4.4).extrude(2.6))
    nut = nut.cut(cyl_z(nx, ny, zb + 0.5, 2.5, 1.7))
    bracket = bracket.union(nut)
# bottom-arm underside raised centre ring
bracket = bracket.union(cyl_z(ARM_CX, ARM_CY, -BZ - 0.8, 0.8, 10.8))
bracket = bracket.cut(cyl_z(ARM_CX, ARM_CY, -BZ - 1.0, 1.2, 6.2))

# ===========================================================================
result = servo.union(bracket)

VIEW = {"azimuth": 45, "elevation": 26}
